import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
flange_d      = 59.0    # flange (collar) diameter
flange_t      = 2.33    # flange thickness
thread_od     = 50.0    # thread crest diameter
thread_root_d = 46.8    # thread root (groove) diameter
thread_len    = 13.6    # threaded length below the flange
crest_w       = 2.36    # width of a crest land
groove_w      = 2.94    # width of a groove
n_grooves     = 2       # grooves, counted up from the bottom crest

head_side     = 26.0    # square drive head, side length
head_h        = 24.2    # head height above the flange
head_r_vert   = 2.4     # rounding of the head's vertical edges
head_r_top    = 2.5     # rounding of the head's top edges
head_wall     = 1.0     # wall thickness of the hollow (cored) head

bore_d        = 43.6    # bore opening in the underside
bore_depth    = 13.9    # bore depth from the bottom face (ceiling height)

# ---------------- derived ----------------
z_flange = thread_len
z_top_flange = thread_len + flange_t
z_head_top = z_top_flange + head_h
pitch = crest_w + groove_w
r_crest, r_root = thread_od / 2, thread_root_d / 2

# ---------------- revolved body: threaded shank + flange ----------------
pts = [(0.0, 0.0), (r_crest, 0.0)]
for i in range(n_grooves):
    z0 = crest_w + i * pitch          # groove bottom
    z1 = z0 + groove_w                # groove top
    pts += [(r_crest, z0), (r_root, z0), (r_root, z1), (r_crest, z1)]
pts += [
    (r_crest, z_flange),
    (flange_d / 2, z_flange),
    (flange_d / 2, z_top_flange),
    (0.0, z_top_flange),
]
body = (
    cq.Workplane("XZ").polyline(pts).close()
    .revolve(360, (0, 0, 0), (0, 1, 0))
    .rotate((0, 0, 0), (0, 0, 1), 90)   # park the revolve seam at the back (+Y)
)

# ---------------- square drive head ----------------
head = (
    cq.Workplane("XY").workplane(offset=z_top_flange)
    .rect(head_side, head_side).extrude(head_h)
    .edges("|Z").fillet(head_r_vert)
    .faces(">Z").edges().fillet(head_r_top)
)
body = body.union(head)

# ---------------- plain bore in the underside ----------------
bore = (
    cq.Workplane("XY").workplane(offset=-1.0)
    .circle(bore_d / 2).extrude(bore_depth + 1.0)
)
body = body.cut(bore)

# ---------------- core of the head: inward offset of the head by head_wall ----------------
core_side = head_side - 2 * head_wall
core_top = z_head_top - head_wall
core_z0 = bore_depth - 0.5
core = (
    cq.Workplane("XY").workplane(offset=core_z0)
    .rect(core_side, core_side).extrude(core_top - core_z0)
    .edges("|Z").fillet(head_r_vert - head_wall)
    .faces(">Z").edges().fillet(head_r_top - head_wall)
)
result = body.cut(core)

VIEW = {"azimuth": 45, "elevation": 26}
